import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
L = 300.0      # length along Y (incl. frame / tab at -Y end)
D = 94.0       # depth along X (back at X=0, open front at X=D)
H = 166.0      # height along Z (open top)

YS = 13.6      # body -Y face offset (frame & tab stick out to Y=0)
YE = 0.8       # body +Y face inset from the frame
R1 = 68.0      # plan radius of the back / -Y corner
R2 = 0.0       # plan radius of the back / +Y corner (sharp)
ZB = 1.5       # body bottom sits slightly above frame bottom
T = 4.0        # general wall thickness
TF = 5.0       # floor top (inside) height
TY = 5.0       # +Y end wall thickness
TY_LIP = 9.5   # +Y end wall thickness at the top lip
LIP_H = 7.0    # height of that top lip
FD = 20.0      # frame depth (X) at the open front
FW = 8.5       # frame face width (sides)
FWB = 6.5      # frame face width (bottom)
FIN = 10.0     # inward projection of the pads on the +Y frame side
FR = 10.0      # frame outer bottom corner radius
LIP_D = 7.0    # depth (X) of the raised lip at the front edge of the floor
RB = 4.0       # body bottom edge fillet
RBEAD = 13.0   # rounded top-back edge (bead)

BAND_H = 10.0      # interior top band height
ELB_H = 29.0       # elbow depth where it ends (short of the tab)
ELB_X = 10.0       # elbow ends where the outer curve reaches this X
GAP_X = 25.3       # the gap behind the elbow end stops at this X
GAP_W = 3.0        # thickness of the plate closing the gap towards the open front
GAP_Y0, GAP_Y1 = 31.0, 46.0   # Y span of that plate
BAND_X = 23.0      # interior band / block front face (from back outer face)
BLK_Y0 = 239.0     # interior block start (Y)
BLK_Z0 = 131.6     # interior block bottom (Z)
RIB_Y0, RIB_Y1 = 129.0, 263.0
RIB_T = 3.8
RIB_X = 16.0

TAB_X0 = 36.0      # tab at the -Y end (top, front half)
TAB_H = 30.0
TAB_RC = 2.0       # plan radius of the tab's back/-Y corner
TAB_LEAN = 0.0     # tab back face lean (X offset at the top)

NOTCH_X = 12.0     # notch at back/top/+Y corner
NOTCH_W = 44.0
NOTCH_H = 30.0
SLOT_Y, SLOT_Z = 277.0, 154.0   # slot in the notch face

PLATE_X = 14.0     # X length of the inner pads on the +Y frame side
PLATE_H = 56.0     # height of the lower pad
CLIP_H = 12.0      # height of the top clip

SYM_X, SYM_Z = 63.0, 118.0   # raised contactless symbol on the +Y face
SYM_R = (11.0, 15.0, 19.5)


def plan_profile(x0, y0, x1, y1, r1, r2):
    """Plan (XY) outline: rectangle with rounded back corners."""
    c = math.cos(math.radians(45.0))
    wp = cq.Workplane("XY").moveTo(x1, y0).lineTo(x1, y1)
    if r2 > 0:
        wp = wp.lineTo(x0 + r2, y1).threePointArc((x0 + r2 - r2 * c, y1 - r2 + r2 * c), (x0, y1 - r2))
    else:
        wp = wp.lineTo(x0, y1)
    wp = (
        wp.lineTo(x0, y0 + r1)
        .threePointArc((x0 + r1 - r1 * c, y0 + r1 - r1 * c), (x0 + r1, y0))
        .close()
    )
    return wp


def box(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False).translate((x0, y0, z0))


# ---------------- outer body ----------------
body = plan_profile(0.0, YS, D, L - YE, R1, R2).extrude(H - ZB).translate((0, 0, ZB))
body = body.edges("<Z").fillet(RB)

# rounded top/back bead (back face + curved corner + -Y side, hidden under the tab)
body = body.edges(
    cq.selectors.BoxSelector((-1, YS + R1 + 1, H - 1), (1.0, L - 1, H + 1))
).fillet(RBEAD)

# notch at back / top / +Y corner
notch = box(-5, NOTCH_X, L - NOTCH_W, L + 5, H - NOTCH_H, H + 5)
notch = notch.edges("|Z and >X and <Y").fillet(5.0)
notch = notch.edges("|X and <Z and <Y").fillet(4.0)
body = body.cut(notch)

# gap in the curved wall top between the end of the elbow and the tab
_c0, _c1 = R1, YS + R1
_p0 = math.pi + math.acos((R1 - ELB_X) / R1)
_p1 = math.pi + math.acos((R1 - GAP_X - 6.0) / R1)
_pm = 0.5 * (_p0 + _p1)


def _gp(r, a):
    return (_c0 + r * math.cos(a), _c1 + r * math.sin(a))


gap = (
    cq.Workplane("XY", origin=(0, 0, H - ELB_H))
    .moveTo(*_gp(R1 + 3.0, _p0))
    .threePointArc(_gp(R1 + 3.0, _pm), _gp(R1 + 3.0, _p1))
    .lineTo(*_gp(R1 - T - 3.0, _p1))
    .threePointArc(_gp(R1 - T - 3.0, _pm), _gp(R1 - T - 3.0, _p0))
    .close()
    .extrude(ELB_H + 2)
).intersect(box(-10.0, GAP_X, 0.0, L, H - ELB_H - 1, H + 5))
body = body.cut(gap)

# ---------------- front frame ----------------
frame = box(D - FD, D, 0, L, 0, H)
frame = frame.edges("|X and <Z").fillet(FR)
frame = frame.edges("|X and >Z").fillet(2.0)

# ---------------- tab at -Y end ----------------
tab = (
    cq.Workplane("XZ", origin=(0, 0, 0))
    .polyline([(TAB_X0, H - TAB_H), (D - FD + 1, H - TAB_H), (D - FD + 1, H), (TAB_X0 + TAB_LEAN, H)])
    .close()
    .extrude(-(YS + 20))
)
tab = tab.edges("|Z and <X and <Y").fillet(TAB_RC)
tab = tab.edges("<Z").fillet(6.0)
tab = tab.edges(">Z and (not |Y)").fillet(4.0)

solid = body.union(frame).union(tab)

# ---------------- interior cavity (keeps the top band, block and elbow) ----------------
cav = (
    plan_profile(T, YS + T, D - FD, L - YE - TY, R1 - T, 0.0)
    .extrude(H)
    .translate((0, 0, TF))
)

band = box(0, BAND_X, YS + R1 - 0.5, BLK_Y0 + 0.5, H - BAND_H, H + 2)
block = box(0, BAND_X, BLK_Y0, L, BLK_Z0, H + 2)
# elbow: annular sector of the band following the curved corner, ending short of the tab
cx, cy = R1, YS + R1
phi_end = math.acos((R1 - ELB_X) / R1)
ri_ = R1 - BAND_X


def _pt(r, a):
    return (cx + r * math.cos(a), cy + r * math.sin(a))


a0, a1 = math.pi, math.pi + phi_end
am = 0.5 * (a0 + a1)
ring = (
    cq.Workplane("XY", origin=(0, 0, H - ELB_H))
    .moveTo(*_pt(R1 + 1.0, a0))
    .threePointArc(_pt(R1 + 1.0, am), _pt(R1 + 1.0, a1))
    .lineTo(*_pt(ri_, a1))
    .threePointArc(_pt(ri_, am), _pt(ri_, a0))
    .close()
    .extrude(ELB_H)
)
ring = ring.faces(">Z").edges(cq.selectors.RadiusNthSelector(0)).fillet(8.0)
# sloped underside: BAND_H deep where it meets the straight band, ELB_H deep at the tab
y_hi, y_lo = cy, _pt(R1, a1)[1]
slope = (ELB_H - BAND_H) / (y_hi - y_lo)
under = (
    cq.Workplane("YZ", origin=(-5, 0, 0))
    .polyline(
        [
            (y_hi + 5, H - BAND_H + 5 * slope),
            (y_lo - 20, H - ELB_H - 20 * slope),
            (y_lo - 20, H - ELB_H - 60),
            (y_hi + 5, H - ELB_H - 60),
        ]
    )
    .close()
    .extrude(D + 10)
)
ring = ring.cut(under)
cav = cav.cut(band).cut(block).cut(ring)
solid = solid.cut(cav)

# frame opening with a raised lip at the front edge of the floor and a shallow recess around it
solid = solid.cut(box(D - FD - 1, D + 1, YS + T - 0.6, L - FW, TF, H + 1))
lip = box(D - LIP_D, D - 1.0, YS + T - 1.0, L - FW + 0.5, TF - 0.5, FWB + 2.0)
lip = lip.edges("|Y and >Z and <X").fillet(3.5)
solid = solid.union(lip)
solid = solid.cut(box(D - 2.0, D + 1, FW, L - FW, FWB, H + 1))

# +Y wall top lip; inner thickenings of the +Y frame side (lower pad and top clip)
solid = solid.union(box(NOTCH_X, D - FD, L - YE - TY_LIP, L - YE - TY + 0.1, H - LIP_H, H))
solid = solid.union(box(D - FD, D - FD + PLATE_X, L - FW - FIN, L - FW + 0.1, TF - 0.1, TF + PLATE_H))
solid = solid.union(box(D - FD, D - FD + PLATE_X, L - FW - FIN, L - FW + 0.1, H - CLIP_H, H))

# plate behind the elbow end, continuing the wall next to the tab (faces the open front)
solid = solid.union(box(GAP_X - GAP_W, GAP_X, GAP_Y0, GAP_Y1, H - ELB_H, H))

# rib under the recess
rib = box(T - 0.5, RIB_X, RIB_Y0, RIB_Y1, BLK_Z0 - RIB_T, BLK_Z0)
rib = rib.edges("|X and >Y").fillet(1.8)
solid = solid.union(rib)

# ---------------- raised contactless symbol on the +Y face ----------------
SYM_W, SYM_T, SYM_A = 2.0, 1.0, 45.0
ys0 = L - YE - 0.1


def _arc_band(r, a_mid):
    """Raised arc band of mean radius r centred on the symbol, spanning a_mid +/- SYM_A (deg, in the XZ plane)."""
    ro, ri = r + SYM_W / 2, r - SYM_W / 2
    a0, a1 = math.radians(a_mid - SYM_A), math.radians(a_mid + SYM_A)
    am = math.radians(a_mid)

    def p(rr, a):
        return (SYM_X + rr * math.cos(a), SYM_Z + rr * math.sin(a))

    return (
        cq.Workplane("XZ", origin=(0, ys0, 0))
        .moveTo(*p(ro, a0))
        .threePointArc(p(ro, am), p(ro, a1))
        .lineTo(*p(ri, a1))
        .threePointArc(p(ri, am), p(ri, a0))
        .close()
        .extrude(-(SYM_T + 0.1))
    )


sym = (
    cq.Workplane("XZ", origin=(0, ys0, 0))
    .center(SYM_X, SYM_Z)
    .circle(3.0)
    .circle(1.7)
    .extrude(-(SYM_T + 0.1))
)
for r in SYM_R:
    for a_mid in (95.0, -85.0):
        sym = sym.union(_arc_band(r, a_mid))
solid = solid.union(sym)

# ---------------- holes / slots ----------------
# slot + two screw holes in the notch face (blind)
solid = solid.cut(
    cq.Workplane("YZ", origin=(NOTCH_X - 1, 0, 0))
    .center(SLOT_Y, SLOT_Z)
    .slot2D(28, 5)
    .extrude(5)
)
solid = solid.cut(
    cq.Workplane("YZ", origin=(NOTCH_X - 1, 0, 0))
    .pushPoints([(SLOT_Y - 13.0, SLOT_Z + 7.5), (SLOT_Y + 3.5, SLOT_Z - 8.5)])
    .circle(1.2)
    .extrude(6)
)
# screw holes in the block front face
solid = solid.cut(
    cq.Workplane("YZ", origin=(BAND_X + 1, 0, 0))
    .pushPoints([(262.0, 160.0), (281.0, 146.0)])
    .circle(1.6)
    .extrude(-12)
)
# holes on the top of the back bead
solid = solid.cut(
    cq.Workplane("XY", origin=(0, 0, H + 1))
    .pushPoints([(12.0, 88.0), (12.0, 232.0)])
    .circle(1.5)
    .extrude(-10)
)
# small holes on the frame tops
solid = solid.cut(
    cq.Workplane("XY", origin=(0, 0, H + 1))
    .pushPoints([(D - 6.0, 4.5), (D - 6.0, L - 4.5)])
    .circle(1.3)
    .extrude(-8)
)
# parting groove along the tab / frame -Y face
solid = solid.cut(box(48.0, D - 7.0, -1.0, 0.5, H - 5.4, H - 4.6))
# square hole in the tab back face
solid = solid.cut(box(TAB_X0 - 5, TAB_X0 + 8, 9.0, 15.0, H - 19, H - 13))

result = solid
